import cadquery as cq

# ---- driving dimensions (mm) ----
R_OUT = 40.0        # body outer radius
H_BODY = 33.25      # body height (bottom to shoulder)
H_NECK = 3.65       # threaded neck height above shoulder
R_TIP = 38.0        # thread crest (tip) radius
R_ROOT = 37.1       # thread root / neck core radius
R_BORE = 35.25      # inner bore radius
T_FLOOR = 8.3       # floor (bottom wall) thickness
PITCH = 1.33        # thread pitch
TIP0 = 0.15         # height of first crest above the shoulder
N_TEETH = 3         # thread turns, modelled as plain V-rings
Z_OUT_SPLIT = 29.5  # face split line on outer wall
Z_IN_SPLIT = 26.0   # face split line on inner wall
SEAM_ANGLE = 45.0   # rotate revolve seam away from the main view

H_TOT = H_BODY + H_NECK
DEPTH = R_TIP - R_ROOT
HALF = 0.5 * PITCH

# ---- half cross-section (X = radius, Z = height) revolved about Z ----
pts = [(0, 0), (R_OUT, 0), (R_OUT, Z_OUT_SPLIT), (R_OUT, H_BODY)]
# first tooth runs into the shoulder: its lower flank is cut by the shoulder plane
r_start = max(R_ROOT, R_TIP - DEPTH * TIP0 / HALF)
pts.append((r_start, H_BODY))
for i in range(N_TEETH):
    zt = H_BODY + TIP0 + i * PITCH
    pts.append((R_TIP, zt))
    pts.append((R_ROOT, min(zt + HALF, H_TOT)))
if pts[-1][1] < H_TOT:
    pts.append((R_ROOT, H_TOT))
pts += [(R_BORE, H_TOT), (R_BORE, Z_IN_SPLIT), (R_BORE, T_FLOOR), (0, T_FLOOR)]

prof = cq.Workplane("XZ").polyline(pts).close()
body = prof.revolve(360, (0, 0, 0), (0, 1, 0), clean=False)
result = body.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)

VIEW = {"azimuth": 45, "elevation": 26}
